import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
HW = 51.3          # half width of the plan at the base
Y0 = -0.6          # front of the plan at the base
RC = 27.9          # plan radius of the big front corners (they run on past the widest point)
X_ARM_END = 48.2   # |x| of the straight outer side at the end of the long arm (base)
R_KINK = 3.0       # concave blend between the corner arc and that straight side
Y_BACK = 62.0      # construction back of the closed outer plan (cut away later)
R_BACK = 8.0      # construction back corner radius (cut away later)
H = 48.4           # overall height
DRAFT_OUT = 4.0    # outer wall draft (deg)
DRAFT_IN = 6.5     # cavity wall draft (deg)
FLOOR_Z = 10.0     # top of the floor / back ledge
CAV_FRONT_Y = 17.2  # cavity front wall at floor level
CAV_SIDE_X = 34.4   # cavity half width at floor level
CAV_BACK_Y = 34.2   # cavity back wall at floor level (opened by the back slot)
CAV_RC = 8.0        # cavity front corner radius at floor level
CAV_RB = 3.2        # cavity back corner radius at floor level
SLOT_X = -31.7      # flat inner face of the long arm at floor level
R_BOT = 9.5        # bottom edge fillet
R_TOP_OUT = 8.0    # outer rim fillet
R_TOP_IN = 1.0     # inner rim fillet

# back opening (plan steps)
D_END = 42.4       # back end of the long (-X) arm
X_STEP_L = -25.9   # long-arm foot inner edge
X_STEP_R = 24.8    # ledge end toward the short arm
Y_LEDGE = 35.3     # back face of the ledge
Y_SHORT = 31.0     # end of the short (+X) arm
R_STEP = 1.5       # small rounding of the ledge step
R_END = 1.0        # small rounding of the cut arm ends

# front wall holes (X, Z)
HOLE_D = 4.2
HOLES = [(-24.5, 39.1), (-12.7, 39.1), (0.0, 39.1), (13.8, 39.1), (26.0, 39.1),
         (-22.2, 28.9), (23.7, 28.0),
         (-20.7, 17.0), (-6.0, 17.0), (7.4, 17.0), (21.7, 17.0)]

# inner rectangular recess on the front wall (X range, Z range, depth)
REC_X = (-14.2, 13.8)
REC_Z = (21.0, 34.7)
REC_DEPTH = 1.4

# floor features
PIN_D = 3.8
PIN_H = 2.8
PIN_CH = 0.9
PIN_XY = [(-14.0, 32.0), (14.0, 32.0)]
FLOOR_HOLE_D = 3.7
FLOOR_HOLE_XY = (0.0, 32.0)
LIP_D = 4.4              # thin lip around the floor hole on the underside
LIP_H = 0.35
POCKET_DEPTH = 5.0
POCKET_Y_TOP = 30.0      # straight back edge of the D pockets
POCKET_X_IN = 11.9       # straight inner edge of the D pockets
POCKET_Y_IN = 19.0       # lower end of the inner edge
POCKET_C = (24.5, 27.5)  # centre of the round part (|x|, y)
POCKET_R = 9.8
POCKET_X_NOTCH = 17.7    # |x| where the notch meets the round part


def outer_plan():
    """Closed outer plan at the base: straight front, big round corners that
    carry on past the widest point, a small concave blend into the straight
    ends of the arms and a construction back (cut away later)."""
    xc = HW - RC
    yc = Y0 + RC
    # concave blend circle, tangent to the corner circle and to x = X_ARM_END
    bx = X_ARM_END + R_KINK
    by = yc + math.sqrt((RC + R_KINK) ** 2 - (bx - xc) ** 2)
    d = math.hypot(bx - xc, by - yc)
    t1 = (xc + RC * (bx - xc) / d, yc + RC * (by - yc) / d)     # on the corner arc
    t2 = (X_ARM_END, by)                                         # on the straight side
    a1 = math.atan2(t1[1] - by, t1[0] - bx) % (2 * math.pi)
    a2 = math.pi
    km = (bx + R_KINK * math.cos((a1 + a2) / 2), by + R_KINK * math.sin((a1 + a2) / 2))
    a_t = math.atan2(t1[1] - yc, t1[0] - xc)
    a_m = (a_t - math.pi / 2) / 2
    cm = (xc + RC * math.cos(a_m), yc + RC * math.sin(a_m))
    yb_c = Y_BACK - R_BACK
    xb = X_ARM_END - R_BACK
    bm = (xb + R_BACK * math.cos(math.pi / 4), yb_c + R_BACK * math.sin(math.pi / 4))
    wp = (cq.Workplane("XY").moveTo(-xc, Y0).lineTo(xc, Y0)
          .threePointArc(cm, t1)
          .threePointArc(km, t2)
          .lineTo(X_ARM_END, yb_c)
          .threePointArc(bm, (xb, Y_BACK))
          .lineTo(-xb, Y_BACK)
          .threePointArc((-bm[0], bm[1]), (-X_ARM_END, yb_c))
          .lineTo(-t2[0], t2[1])
          .threePointArc((-km[0], km[1]), (-t1[0], t1[1]))
          .threePointArc((-cm[0], cm[1]), (-xc, Y0))
          .close())
    return wp.wires().val()


def cavity_plan(z):
    """Cavity plan at floor level: rounded rectangle (big front corners,
    small back corners)."""
    w = 2 * CAV_SIDE_X
    d = CAV_BACK_Y - CAV_FRONT_Y
    yc = (CAV_BACK_Y + CAV_FRONT_Y) / 2
    sk = (cq.Sketch()
          .push([(0, yc)]).rect(w, d)
          .reset()
          .vertices("<Y").fillet(CAV_RC)
          .reset()
          .vertices(">Y").fillet(CAV_RB))
    return (cq.Workplane("XY", origin=(0, 0, z)).placeSketch(sk))


# ---------------- outer body ----------------
body = cq.Workplane("XY").add(outer_plan()).toPending().extrude(H, taper=DRAFT_OUT)
body = body.edges("<Z").fillet(R_BOT)

# ---------------- drafted cavity, open at the back ----------------
cav_h = H - FLOOR_Z + 8.0
cavity = cavity_plan(FLOOR_Z).extrude(cav_h, taper=-DRAFT_IN)
body = body.cut(cavity)

# open the cavity toward the back above the floor; the cut face is the flat,
# drafted inner face at the end of the long arm
tz = math.tan(math.radians(DRAFT_IN))
z_top = H + 10.0
back_slot = (cq.Workplane("XZ", origin=(0, 0, 0))
             .polyline([(SLOT_X, FLOOR_Z), (80.0, FLOOR_Z), (80.0, z_top),
                        (SLOT_X - (z_top - FLOOR_Z) * tz, z_top)]).close()
             .extrude(-80.0)
             .translate((0, Y_SHORT, 0)))
body = body.cut(back_slot)

# ---------------- open back (stepped plan cut) ----------------
BIG = 80.0
back_cut = (cq.Workplane("XY", origin=(0, 0, -5))
            .polyline([(-BIG, D_END), (X_STEP_L, D_END), (X_STEP_L, Y_LEDGE),
                       (X_STEP_R, Y_LEDGE), (X_STEP_R, Y_SHORT), (BIG, Y_SHORT),
                       (BIG, BIG), (-BIG, BIG)]).close()
            .extrude(H + 10))
body = body.cut(back_cut)


def edges_near(wp, pts, tol=0.3):
    """Edges of wp whose centre lies within tol of one of the given points."""
    out = []
    for e in wp.edges().vals():
        c = e.Center()
        for p in pts:
            if abs(c.x - p[0]) < tol and abs(c.y - p[1]) < tol and abs(c.z - p[2]) < tol:
                out.append(e)
                break
    return out


# soften the stepped ledge / foot at the back
step_pts = [(X_STEP_L, (Y_LEDGE + D_END) / 2, FLOOR_Z),
            (X_STEP_L, D_END, FLOOR_Z / 2),
            (X_STEP_L, Y_LEDGE, FLOOR_Z / 2),
            (X_STEP_R, Y_LEDGE, FLOOR_Z / 2),
            (X_STEP_R, Y_SHORT, FLOOR_Z / 2),
            ((X_STEP_L + X_STEP_R) / 2, Y_LEDGE, FLOOR_Z),
            (X_STEP_R, (Y_SHORT + Y_LEDGE) / 2, FLOOR_Z)]
body = body.newObject(edges_near(body, step_pts)).fillet(R_STEP)


def rim_edges(wp):
    """Split the edges of the top (rim) face into outer and inner chains,
    leaving out the short edges on the cut arm ends."""
    face = wp.faces(">Z").val()
    outer, inner = [], []
    for e in face.Edges():
        c = e.Center()
        if e.geomType() == "LINE" and (abs(c.y - D_END) < 0.1 or abs(c.y - Y_SHORT) < 0.1):
            continue
        # the outer chain lies closer to the part's outside than the cavity does
        p = c
        if e.geomType() == "LINE":
            is_outer = p.y < (Y0 + CAV_FRONT_Y) / 2.0
        else:
            is_outer = abs(p.x) > (HW + CAV_SIDE_X) / 2.0 + 2.0 or (p.y < CAV_FRONT_Y - 6.0)
        (outer if is_outer else inner).append(e)
    return outer, inner


# ---------------- rounded rim ----------------
outer_e, inner_e = rim_edges(body)
inner_c = [e.Center() for e in inner_e]
body = body.newObject(outer_e).fillet(R_TOP_OUT)
inner_e = [e for e in body.faces(">Z").val().Edges()
           if any((e.Center() - c).Length < 1e-3 for c in inner_c)]
body = body.newObject(inner_e).fillet(R_TOP_IN)

# ---------------- softened arm ends ----------------
def arm_end_edges(wp):
    """Profile edges of the two cut arm ends (above the floor / outside the foot)."""
    sel = []
    for f in wp.faces().vals():
        if f.geomType() != "PLANE":
            continue
        n = f.normalAt()
        bb = f.BoundingBox()
        long_end = abs(bb.ymin - D_END) < 1e-3 and bb.xmax < X_STEP_L + 1e-3
        short_end = abs(bb.ymin - Y_SHORT) < 1e-3 and bb.xmin > X_STEP_R - 1e-3
        if abs(n.y - 1) < 1e-6 and (long_end or short_end):
            for e in f.Edges():
                c = e.Center()
                if c.z > FLOOR_Z + 0.5 or (c.z > 0.5 and abs(c.x) > 40):
                    sel.append(e)
    return sel


body = body.newObject(arm_end_edges(body)).fillet(R_END)

# ---------------- floor features ----------------
def d_pocket(sign):
    """D-shaped floor pocket: straight back and inner edges, a small notch,
    and a round outer part that follows the cavity corner."""
    s = sign
    cx, cy = POCKET_C
    r = POCKET_R
    # point on the round part where the notch meets it
    xn = POCKET_X_NOTCH
    yn = cy - math.sqrt(r ** 2 - (cx - xn) ** 2)
    x_left = cx + math.sqrt(r ** 2 - (POCKET_Y_TOP - cy) ** 2)
    pts = [(s * POCKET_X_IN, POCKET_Y_TOP), (s * POCKET_X_IN, POCKET_Y_IN), (s * xn, yn)]
    wp = (cq.Workplane("XY", origin=(0, 0, FLOOR_Z - POCKET_DEPTH))
          .moveTo(*pts[0]).lineTo(*pts[1]).lineTo(*pts[2])
          .threePointArc((s * cx, cy - r), (s * x_left, POCKET_Y_TOP))
          .close())
    return wp.extrude(POCKET_DEPTH + 1.0)


for sgn in (-1, 1):
    body = body.cut(d_pocket(sgn))

for (px, py) in PIN_XY:
    pin = (cq.Workplane("XY", origin=(px, py, FLOOR_Z - 0.5))
           .circle(PIN_D / 2).extrude(PIN_H + 0.5)
           .faces(">Z").edges().chamfer(PIN_CH))
    body = body.union(pin)

lip = (cq.Workplane("XY", origin=(FLOOR_HOLE_XY[0], FLOOR_HOLE_XY[1], -LIP_H))
       .circle(LIP_D / 2).extrude(LIP_H + 0.5))
body = body.union(lip)

floor_hole = (cq.Workplane("XY", origin=(FLOOR_HOLE_XY[0], FLOOR_HOLE_XY[1], -1))
              .circle(FLOOR_HOLE_D / 2).extrude(FLOOR_Z + 2))
body = body.cut(floor_hole)

# ---------------- front wall holes ----------------
for (hx, hz) in HOLES:
    cyl = cq.Solid.makeCylinder(HOLE_D / 2, 30.0, cq.Vector(hx, -5.0, hz), cq.Vector(0, 1, 0))
    body = body.cut(cq.Workplane("XY").add(cyl))

# ---------------- rectangular recess on the inside of the front wall ----------------
t = math.tan(math.radians(DRAFT_IN))
y_in_floor = CAV_FRONT_Y
zc = (REC_Z[0] + REC_Z[1]) / 2
yc_face = y_in_floor - (zc - FLOOR_Z) * t
rec = (cq.Workplane("XY")
       .box(REC_X[1] - REC_X[0], 2 * REC_DEPTH, REC_Z[1] - REC_Z[0])
       .rotate((0, 0, 0), (1, 0, 0), DRAFT_IN)
       .translate(((REC_X[0] + REC_X[1]) / 2, yc_face, zc)))
body = body.cut(rec)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
